import cadquery as cq

# ---------------------------------------------------------------------------
# Round puck / spacer disk with a central through hole.
# Axis along Y: the two flat faces look to the front (-Y) and back (+Y).
# ---------------------------------------------------------------------------

# Driving dimensions (mm)
DIAMETER = 60.0        # outer diameter of the disk
THICKNESS = 16.2       # axial thickness (along Y)
EDGE_FILLET = 6.25     # rounding of the two outer rims (front and back)
HOLE_D = 9.7           # central through hole

# Purely cosmetic: angular position (about Y) of the closed-surface seams,
# turned away from the default viewing direction.  The solid is axisymmetric,
# so this does not change the shape.
OUTER_SEAM_ROT = 145.0
HOLE_SEAM_ROT = -35.0

# Solid disk, centred on the origin (XZ workplane normal is -Y)
disk = (
    cq.Workplane("XZ")
    .workplane(offset=-THICKNESS / 2.0)
    .circle(DIAMETER / 2.0)
    .extrude(THICKNESS)
)

# Round both outer rims
disk = disk.edges("%CIRCLE").fillet(EDGE_FILLET)
disk = disk.rotate((0, 0, 0), (0, 1, 0), OUTER_SEAM_ROT)

# Central through hole along the axis
hole = (
    cq.Workplane("XZ")
    .workplane(offset=-THICKNESS)
    .circle(HOLE_D / 2.0)
    .extrude(2.0 * THICKNESS)
    .rotate((0, 0, 0), (0, 1, 0), HOLE_SEAM_ROT)
)

result = disk.cut(hole)

VIEW = {"azimuth": 45, "elevation": 26}
